import cadquery as cq

# =====================================================================
#  Chimney / vent pipe on a square roof plate.
#  Casing section: "pillowed square" = sharp square corners, every side
#  bulged outward by a circular arc; it tapers in at the bulges and flares
#  out at the corners going up (one ruled loft).  Lower pipe: single skin
#  with a round-cornered bore.  Storm collar: square corner angles + a
#  rounded-square bore, capped by a square flange.  Upper pipe: double
#  wall (skin + inner liner) with the air gap open at the rim.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
PLATE_HALF = 250.0      # square base plate, half width
PLATE_T = 6.0           # base plate thickness
BODY_H = 701.0          # casing height above the base plate

R_BOT = 212.0           # casing: distance axis -> crown of each bulged side, at the base
R_TOP = 198.5           # ... at the top (casing tapers inward)
S_BOT = 163.5           # casing square corners, half width at the base
S_TOP = 172.5           # ... at the top (corners flare outward)
A_BOT = 122.0           # half length of the bulged arc along a side, at the base
A_TOP = 120.0           # ... at the top
SKIN_T = 5.0            # casing sheet thickness
GAP = 6.5               # upper pipe: air gap between casing and inner liner
LINER_T = 8.0           # upper pipe: inner liner wall thickness
LINER_CR = 30.0         # upper pipe: corner radius of the liner bore

STEP_Z = 168.0          # bottom of the storm collar (above plate top)
FLANGE_Z = 516.5        # flange underside = collar top (above plate top)
FLANGE_HALF = 212.0     # flange half width
FLANGE_T = 7.0          # flange thickness
COLLAR_S = 177.0        # storm collar: half width of its square corner angles
COLLAR_A = 123.0        # storm collar: corner angles end this far from the side centre
BORE_HALF = 170.0       # storm collar bore: flat half width (rounded square)
BORE_R = 84.0           # storm collar bore: corner radius

VIEW = {"azimuth": 45, "elevation": 26}

Z0 = PLATE_T                    # casing starts on the plate
Z1 = PLATE_T + BODY_H           # top rim
ZS = Z0 + STEP_Z                # collar bottom
ZF = Z0 + FLANGE_Z              # collar top / flange underside
E = 15.0                        # overshoot for cutting tools


def lerp(a, b, f):
    return a + (b - a) * f


def par(z):
    """Casing section parameters (bulge R, corner half width s, arc half length a) at height z."""
    f = (z - Z0) / BODY_H
    return lerp(R_BOT, R_TOP, f), lerp(S_BOT, S_TOP, f), lerp(A_BOT, A_TOP, f)


def pillow_wire(z, off=0.0, corner_r=0.0):
    """Pillowed square: square corners (optionally rounded by corner_r), each side bulged
    by a 3-point arc; all sides moved outward by off (negative = inward)."""
    R, s, a = par(z)
    R, s, a = R + off, s + off, a + off     # keep the flat corner length constant
    w = (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(s, s).lineTo(a, s).threePointArc((0, R), (-a, s)).lineTo(-s, s)
        .lineTo(-s, a).threePointArc((-R, 0), (-s, -a)).lineTo(-s, -s)
        .lineTo(-a, -s).threePointArc((0, -R), (a, -s)).lineTo(s, -s)
        .lineTo(s, -a).threePointArc((R, 0), (s, a)).close()
        .wire().val()
    )
    if corner_r > 0:
        corners = [v for v in w.Vertices() if abs(abs(v.X) - s) < 1e-6 and abs(abs(v.Y) - s) < 1e-6]
        w = w.fillet2D(corner_r, corners)
    return w


def casing(z0, z1, off=0.0, corner_r=0.0):
    """Ruled loft of the casing section between z0 and z1 (offset by off)."""
    return cq.Workplane("XY").add(
        cq.Solid.makeLoft([pillow_wire(z0, off, corner_r), pillow_wire(z1, off, corner_r)], True)
    )


def round_bore(z0, z1, off):
    """Round bore following the casing bulge radius (clips the bore corners round)."""
    r0, r1 = par(z0)[0] + off, par(z1)[0] + off
    return cq.Workplane("XY").add(
        cq.Solid.makeCone(r0, r1, z1 - z0, cq.Vector(0, 0, z0), cq.Vector(0, 0, 1)))


def box(half, z0, z1):
    return cq.Workplane("XY", origin=(0, 0, z0)).rect(2 * half, 2 * half).extrude(z1 - z0)


def rsq(half, rad, z0, z1):
    """Rounded-square prism."""
    w = cq.Workplane("XY", origin=(0, 0, z0)).rect(2 * half, 2 * half).val()
    face = cq.Face.makeFromWires(w.fillet2D(rad, w.Vertices()))
    return cq.Workplane("XY").add(cq.Solid.extrudeLinear(face, cq.Vector(0, 0, z1 - z0)))


def zbox(z0, z1, half=400.0):
    return box(half, z0, z1)


def cross(c, z0, z1):
    """Plus-shaped prism: |x| < c or |y| < c."""
    return (cq.Workplane("XY", origin=(0, 0, z0)).rect(2 * c, 800.0).extrude(z1 - z0)
            .union(cq.Workplane("XY", origin=(0, 0, z0)).rect(800.0, 2 * c).extrude(z1 - z0)))


# ---------------- casing surfaces (one ruled loft each, full height) ----------------
OUT = casing(Z0, Z1)                                            # casing outside
SKIN_IN = casing(Z0 - E, Z1 + E, -SKIN_T)                       # casing inside
LINER_OUT = casing(Z0 - E, Z1 + E, -(SKIN_T + GAP))             # upper liner outside
LINER_IN = casing(Z0 - E, Z1 + E, -(SKIN_T + GAP + LINER_T), LINER_CR)  # upper liner bore

# ---------------- solid envelope: casing + collar corners + flange + base plate ----------------
envelope = (
    OUT.union(box(COLLAR_S, ZS, ZF).cut(cross(COLLAR_A, ZS - 1.0, ZF + 1.0)))   # storm collar corner angles
    .union(box(FLANGE_HALF, ZF, ZF + FLANGE_T)                  # collar flange (square ring)
           .cut(box(COLLAR_S, ZF - 1.0, ZF + FLANGE_T + 1.0)))
    .union(box(PLATE_HALF, 0.0, PLATE_T))                       # base plate
)

# ---------------- cavities ----------------
bore_lower = (SKIN_IN.intersect(zbox(-E, ZS))                   # lower pipe bore (single skin) + plate hole,
              .intersect(round_bore(-E, ZS + E, -SKIN_T)))       # corners rounded by the bulge circle
bore_collar = rsq(BORE_HALF, BORE_R, ZS - 1.0, ZF + 1.0)        # rounded-square collar bore
air_gap = (SKIN_IN.cut(LINER_OUT)                               # double-wall air gap,
           .intersect(zbox(ZF + FLANGE_T, Z1 + E)))             # open at the rim
bore_upper = LINER_IN.intersect(zbox(ZF - 1.0, Z1 + E))         # upper liner bore
plate_recess = casing(-E, 1.0)                                  # casing footprint recessed 1 mm into the plate underside
cavity = bore_lower.union(plate_recess).union(bore_collar).union(air_gap).union(bore_upper)

result = envelope.cut(cavity)
